import math
import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_NurbsConvert, BRepBuilderAPI_GTransform
from OCP.gp import gp_GTrsf, gp_Mat
from OCP.TopoDS import TopoDS

# Pair of identical "63x32" crowned tyre wheels on a common axle line (X axis),
# each with flat side faces, a hub recess on both sides, an axle bore, 30 deg
# side cones and a circular-arc crowned tread, plus raised sidewall lettering.

# ---------------- driving dimensions (mm) ----------------
D_OUT = 63.0          # tyre outer diameter
W = 32.8              # wheel width (axial)
GAP = 1.85            # gap between the two wheels
D_FACE = 42.5         # outer diameter of the flat side face
CONE_DR = 6.75        # radial height of the side chamfer cone
CONE_ANG = 30.0       # side cone angle measured from the face plane (deg)
D_POCKET = 37.2       # hub recess diameter at the face
D_POCKET_FLOOR = 36.6 # hub recess diameter at its floor (drafted wall)
POCKET_DEPTH = 4.9    # hub recess depth (each side)
D_BORE = 8.0          # axle bore

# embossed sidewall lettering (on both side cones of each wheel)
EMBOSS = 0.4          # letter height above the cone surface
SINK = 0.3            # letter root below the surface (for a clean union)
BOLD = 0.12           # outline growth that makes the stroke heavier
FONT = "/usr/share/fonts/truetype/dejavu/DejaVuSansMono-Bold.ttf"
TEXTS = [
    # text, font size, width stretch, centre radius on the cone,
    # centre angle (deg, 0 = +Y, 90 = +Z), overall length along the arc
    ("YTOP", 5.0, 1.05, 25.55, 180.0, 12.8),
    ("63x32", 4.2, 1.25, 24.8, 0.0, 13.9),
]
CHAR_STRETCH = {"x": 0.8}   # narrower multiplication sign

R = D_OUT / 2.0
RF = D_FACE / 2.0
H = W / 2.0
RC = RF + CONE_DR                                   # radius where cone meets crown
TAN_C = math.tan(math.radians(CONE_ANG))
CONE_DX = CONE_DR * TAN_C
RP = D_POCKET / 2.0
RPF = D_POCKET_FLOOR / 2.0
RB = D_BORE / 2.0


def wheel_body():
    """Tyre + hub as one revolved section (X = axle)."""
    xc = H - CONE_DX
    d = POCKET_DEPTH
    # sketch in the XZ plane, radius drawn towards -Z so the seam sits underneath
    sk = (
        cq.Workplane("XZ")
        .polyline([(-H + d, -RB), (-H + d, -RPF), (-H, -RP), (-H, -RF), (-xc, -RC)])
        .threePointArc((0, -R), (xc, -RC))
        .polyline([(xc, -RC), (H, -RF), (H, -RP), (H - d, -RPF), (H - d, -RB)])
        .close()
    )
    return sk.revolve(360, (0, 0, 0), (1, 0, 0))


# ---------------- lettering helpers ----------------
def nurbs_wire(w):
    """Re-express a wire's edges as plain B-splines (offset curves do not survive STEP)."""
    return cq.Wire(TopoDS.Wire_s(BRepBuilderAPI_NurbsConvert(w.wrapped, True).Shape()))


def xstretch(w, k):
    g = gp_GTrsf()
    g.SetVectorialPart(gp_Mat(k, 0, 0, 0, 1, 0, 0, 0, 1))
    return cq.Wire(TopoDS.Wire_s(BRepBuilderAPI_GTransform(w.wrapped, g, True).Shape()))


def grown(w, dist):
    """Offset a closed planar wire by dist outwards (dist > 0) or inwards (dist < 0)."""
    o = w.offset2D(abs(dist), "arc")[0]
    bigger = o.BoundingBox().DiagonalLength > w.BoundingBox().DiagonalLength
    if bigger != (dist > 0):
        o = w.offset2D(-abs(dist), "arc")[0]
    return nurbs_wire(o)


def glyph(ch, size, k):
    """Heavy, width-stretched glyph as a prism in local XY (baseline along X)."""
    s = cq.Workplane("XY").text(ch, size, 1.0, fontPath=FONT,
                                halign="center", valign="center").val()
    parts = []
    for f in s.Faces():
        if f.normalAt().z > -0.99:          # keep the bottom outline face only
            continue
        outer = grown(xstretch(f.outerWire(), k), BOLD)
        inner = []
        for iw in f.innerWires():
            iw = xstretch(iw, k)
            try:
                inner.append(grown(iw, -BOLD))
            except Exception:
                inner.append(nurbs_wire(iw))
        face = cq.Face.makeFromWires(outer, inner)
        parts.append(cq.Solid.extrudeLinear(face, cq.Vector(0, 0, EMBOSS + SINK)))
    return parts[0] if len(parts) == 1 else cq.Compound.makeCompound(parts)


def cone_plane(r_c, phi_deg):
    """Tangent plane to the +X side cone at radius r_c, angle phi: X along the
    clockwise (seen from +X) circumferential direction, Y up the slope (outwards),
    Z = outward surface normal; origin sunk by SINK."""
    phi = math.radians(phi_deg)
    c = math.radians(CONE_ANG)
    er = cq.Vector(0, math.cos(phi), math.sin(phi))
    et = cq.Vector(0, -math.sin(phi), math.cos(phi))
    n = cq.Vector(math.cos(c), 0, 0) + er * math.sin(c)
    origin = cq.Vector(H - (r_c - RF) * TAN_C, 0, 0) + er * r_c - n * SINK
    return cq.Plane(origin=origin, xDir=-et, normal=n)


def side_letters():
    """Letters of the +X side cone, each set tangent to the cone along the arc."""
    out = []
    for txt, size, k, r_c, phi0, length in TEXTS:
        gl = [glyph(ch, size, k * CHAR_STRETCH.get(ch, 1.0)) for ch in txt]
        bbs = [g.BoundingBox() for g in gl]
        widths = [b.xlen for b in bbs]
        gap = (length - sum(widths)) / (len(txt) - 1)
        ymid = (min(b.ymin for b in bbs) + max(b.ymax for b in bbs)) / 2.0
        s = -length / 2.0
        for g, b, w in zip(gl, bbs, widths):
            sc = s + w / 2.0                     # arc length of the glyph centre
            phi = phi0 - math.degrees(sc / r_c)  # clockwise reading seen from +X
            loc = cq.Location(cone_plane(r_c, phi)) * cq.Location(
                cq.Vector(-(b.xmin + b.xmax) / 2.0, -ymid, 0))
            out.append(g.moved(loc))
            s += w + gap
    return out


def make_wheel():
    body = wheel_body()
    try:
        lets = side_letters()
        # the -X side carries the same lettering, turned half a turn about Y
        flip = cq.Location(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 180)
        both = lets + [s.moved(flip) for s in lets]
        emb = cq.Workplane("XY").newObject([cq.Compound.makeCompound(both)])
        lettered = body.union(emb)
        if lettered.val().isValid():
            body = lettered
    except Exception:
        pass  # lettering is cosmetic; keep the plain wheel if the font is missing
    return body.val()


wheel = make_wheel()
offset = (W + GAP) / 2.0
# two identical wheels side by side on the common axle line (X)
wheels = [wheel.translate(cq.Vector(s * offset, 0, 0)) for s in (-1, 1)]
if not all(w.isValid() for w in wheels):      # safety net: plain wheels
    plain = wheel_body().val()
    wheels = [plain.translate(cq.Vector(s * offset, 0, 0)) for s in (-1, 1)]
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(wheels)])

VIEW = {"azimuth": 45, "elevation": 26}
